import math
import cadquery as cq

# camera used for the main render (default view)
VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
P = 25.0            # hex cell pitch (flat-to-flat of the outer hex / row spacing)
F1 = 21.4           # upper (lip) hex opening, flat-to-flat
F2 = 23.8           # lower (undercut) hex opening, flat-to-flat
T = 8.3             # plate thickness
D1 = 5.3            # depth of the upper opening (lip depth)
H = 16.4            # total height incl. the mounting flanges
TX = 5.9            # thickness of the -X (left) flange
TF = 4.6            # thickness of the front (-Y) flange
FRONT_OFF = 13.9    # front edge distance below the last row centre line
NOTCH_F = 20.2      # size of the open notch at the missing top-right cell
LEFT_EXT = 1.0      # left strip runs slightly past the last row centre line
HOLE_D = 3.4        # mounting hole diameter
CB_D = 6.9          # counterbore diameter (inner side of the flanges)
CB_DEPTH = 1.2      # counterbore depth
HOLE_Z = -H / 2.0   # mounting hole axis height

a = P / math.sqrt(3.0)      # outer hex circum-radius
DX = 1.5 * a                # column spacing
SQ3 = math.sqrt(3.0)

# cells: column -> list of row indices  (column 1 is the left-most)
CELLS = {
    1: [0, 1, 2],
    2: [0, 1, 2, 3],
    3: [0, 1, 2, 3],
    4: [0, 1, 2, 3, 4],
    5: [0, 1, 2, 3, 4],
    6: [0, 1, 2, 3, 4, 5],
    7: [0, 1, 2, 3, 4],
    8: [1, 2, 3, 4, 5],
}
POCKET = (1, 1)      # cell merged with a rectangular slot to the left wall


def cx(c):
    return (c - 1) * DX


def cy(c, k):
    return -k * P + (P / 2.0 if c % 2 == 0 else 0.0)


def hex_pts(x0, y0, flat):
    r = flat / SQ3
    return [(x0 + r * math.cos(math.radians(60 * i)),
             y0 + r * math.sin(math.radians(60 * i))) for i in range(6)]


def prism(pts, z0, z1):
    return (cq.Workplane("XY").workplane(offset=z0)
            .polyline(pts).close().extrude(z1 - z0))


# ---------------- plate outline ----------------
plate = None
for c, ks in CELLS.items():
    for k in ks:
        p = prism(hex_pts(cx(c), cy(c, k), P), -T, 0)
        plate = p if plate is None else plate.union(p)

X_FI = -14.1                    # inner face of the left flange (= pocket wall)
X_LEFT = X_FI - TX
Y_L_TOP = cy(2, 0)
Y_L_BOT = cy(2, 3) - LEFT_EXT     # front end of the left strip / flange
left_rect = prism([(X_LEFT, Y_L_BOT), (cx(2) - a + LEFT_EXT / SQ3, Y_L_BOT),
                   (cx(2) - a, cy(2, 3)), (cx(2) - a, Y_L_TOP),
                   (X_LEFT, Y_L_TOP)], -T, 0)
plate = plate.union(left_rect)

# front region (plate part under the front flange)
Y6 = cy(6, 5)
Y_FRONT = Y6 - FRONT_OFF
X_RIGHT = cx(8) + a


def x_front_edge(y):
    # continuation of the lower-left edge of the outer hex of cell (6,5)
    yb = Y6 - P / 2.0
    return cx(6) - a / 2.0 - (y - yb) / SQ3


front_poly = [(cx(6) - a, Y6), (x_front_edge(Y_FRONT), Y_FRONT),
              (X_RIGHT, Y_FRONT), (X_RIGHT, Y6)]
plate = plate.union(prism(front_poly, -T, 0))

# thickened corner wall where the top cell of the last column is missing:
# the notch at the empty position (8,0) is bounded by a hex of NOTCH_F
xn, yn = cx(8), cy(8, 0)
rn = NOTCH_F / SQ3
yb_n = yn - NOTCH_F / 2.0                       # bottom edge of the notch hex
x_ur = cx(8) + a / 2.0 - (yb_n - cy(8, 1) - P / 2.0) / SQ3
notch_fill = [(cx(7) + a / 2.0, yn),            # top-right corner of cell (7,0)
              (xn - rn, yn),
              (xn - rn / 2.0, yb_n),
              (x_ur, yb_n),
              (cx(8) + a / 2.0, cy(8, 1) + P / 2.0),
              (cx(8) - a / 2.0, cy(8, 1) + P / 2.0)]
plate = plate.union(prism(notch_fill, -T, 0))

# ---------------- flanges ----------------
# left (-X) mounting flange hanging below the plate
left_flange = prism([(X_LEFT, Y_L_BOT), (X_FI, Y_L_BOT),
                     (X_FI, Y_L_TOP), (X_LEFT, Y_L_TOP)], -H, 0)
# front (-Y) mounting flange hanging below the plate
yf = Y_FRONT + TF
front_flange = prism([(x_front_edge(Y_FRONT), Y_FRONT), (X_RIGHT, Y_FRONT),
                      (X_RIGHT, yf), (x_front_edge(yf), yf)], -H, 0)
body = plate.union(left_flange).union(front_flange)

# ---------------- cells ----------------
# every cell: a smaller hex lip at the top (F1, depth D1) over a larger
# hex undercut (F2) running out through the bottom of the plate
for c, ks in CELLS.items():
    for k in ks:
        x0, y0 = cx(c), cy(c, k)
        up = prism(hex_pts(x0, y0, F1), -D1, 1.0)
        lo = prism(hex_pts(x0, y0, F2), -T - 1.0, -D1)
        up = up.cut(front_flange)          # keep the front flange solid
        lo = lo.cut(front_flange)
        body = body.cut(up).cut(lo)

# pocket: cell (1,1) is extended with a rectangular slot up to the inner
# face of the left flange (screw-head clearance for the left hole)
x0, y0 = cx(POCKET[0]), cy(*POCKET)
r1, r2 = F1 / SQ3, F2 / SQ3
slot_up = prism([(X_FI, y0 - F1 / 2), (x0 - r1 / 2, y0 - F1 / 2),
                 (x0 - r1 / 2, y0 + F1 / 2), (X_FI, y0 + F1 / 2)], -D1, 1.0)
slot_lo = prism([(X_FI, y0 - F2 / 2), (x0 - r2 / 2, y0 - F2 / 2),
                 (x0 - r2 / 2, y0 + F2 / 2), (X_FI, y0 + F2 / 2)],
                -T - 1.0, -D1)
body = body.cut(slot_up.union(slot_lo), clean=False)

# ---------------- mounting holes ----------------
# front flange hole (axis along Y) with a counterbore on the inner side,
# the screw head sits inside cell (6,5)
y_in = Y_FRONT + TF
h1 = (cq.Workplane("XZ", origin=(cx(6), Y_FRONT - 1.0, HOLE_Z))
      .circle(HOLE_D / 2.0).extrude(-(TF + 2.0)))
cb1 = (cq.Workplane("XZ", origin=(cx(6), y_in - CB_DEPTH, HOLE_Z))
       .circle(CB_D / 2.0).extrude(-(CB_DEPTH + 1.0)))
# left flange hole (axis along X) with a counterbore on the inner side,
# the screw head sits inside the pocket of cell (1,1)
h2 = (cq.Workplane("YZ", origin=(X_LEFT - 1.0, cy(1, 1), HOLE_Z))
      .circle(HOLE_D / 2.0).extrude(TX + 2.0))
cb2 = (cq.Workplane("YZ", origin=(X_FI - CB_DEPTH, cy(1, 1), HOLE_Z))
       .circle(CB_D / 2.0).extrude(CB_DEPTH + 1.0))
for tool in (h1, cb1, h2, cb2):
    body = body.cut(tool, clean=False)

result = body
